import cadquery as cq
import math

# ---- driving dimensions (mm) ----
D = 30.0            # outer diameter
L = 56.0            # overall length (along Y)
WALL = 0.7          # tube wall thickness
END_T = 0.7         # closed-end (front, -Y) thickness
EDGE_FILLET = 0.35  # fillet on closed-end outer edge
RIB_BASE_W = 2.0    # internal rib width at the bore wall
RIB_TOP_R = 0.65    # radius of the rib's rounded crest
RIB_H = 1.4         # rib height above the bore wall
RIB_COUNT = 4       # internal ribs, equally spaced
RIB_START_ANGLE = 0.0   # deg, first rib on +X
RIB_INSET = 3.0     # distance ribs stop short of the open end

R = D / 2.0
Ri = R - WALL
Y0 = -L / 2.0       # closed end plane
Y1 = L / 2.0        # open end plane


def y_cyl(radius, y_from, y_to, x=0.0, z=0.0):
    """Solid cylinder with axis parallel to Y from y_from to y_to."""
    return cq.Workplane("XY").add(
        cq.Solid.makeCylinder(radius, y_to - y_from,
                              cq.Vector(x, y_from, z), cq.Vector(0, 1, 0)))


# ---- outer body with rounded closed end, bored from the open end ----
body = y_cyl(R, Y0, Y1)
body = body.faces("<Y").edges().fillet(EDGE_FILLET)
bore = y_cyl(Ri, Y0 + END_T, Y1 + 1.0)
shell = body.cut(bore)
# turn the (axisymmetric) shell so its surface seams fall between the ribs
shell = shell.rotate((0, 0, 0), (0, 1, 0), RIB_START_ANGLE + 180.0 / RIB_COUNT + 180.0)

# ---- one rib on the +X wall: tapered sides, rounded crest pointing inward ----
# profile coordinates (u, v): u = inward distance from bore wall, v = tangential
uc = RIB_H - RIB_TOP_R                  # crest arc centre
hb = RIB_BASE_W / 2.0
# tangent point from the base corner (0, -hb) to the crest circle
dx, dy = 0.0 - uc, -hb - 0.0
d = math.hypot(dx, dy)
alpha = math.acos(RIB_TOP_R / d)
base_ang = math.atan2(dy, dx)
cands = []
for sgn in (1.0, -1.0):
    a = base_ang + sgn * alpha
    cands.append((uc + RIB_TOP_R * math.cos(a), RIB_TOP_R * math.sin(a)))
tu, tv = max(cands, key=lambda p: p[0])  # tangent on the outer flank
root = WALL * 0.5                        # bury the root in the wall


def uv(u, v):
    # (u, v) -> local plane coords (x, y); plane x = global X, plane y = global -Z
    return (Ri - u, v)


y_a = Y0 + END_T * 0.8
y_b = Y1 - RIB_INSET
rib_plane = cq.Plane(origin=(0, y_a, 0), xDir=(1, 0, 0), normal=(0, 1, 0))
rib0 = (cq.Workplane(rib_plane)
        .moveTo(*uv(-root, -hb))
        .lineTo(*uv(0.0, -hb))
        .lineTo(*uv(tu, tv))
        .threePointArc(uv(RIB_H, 0.0), uv(tu, -tv))
        .lineTo(*uv(0.0, hb))
        .lineTo(*uv(-root, hb))
        .close()
        .extrude(y_b - y_a))

result = shell
for i in range(RIB_COUNT):
    ang = RIB_START_ANGLE + i * 360.0 / RIB_COUNT
    result = result.union(rib0.rotate((0, 0, 0), (0, 1, 0), ang))

VIEW = {"azimuth": 45, "elevation": 26}
